import math
import cadquery as cq

# ======================= driving dimensions (mm) =======================
T = 3.0                      # plate thickness
Y_TOP = 59.15                # +Y end edge
Y_BOT = -59.2                # -Y end edge
BODY_HALF_W = 21.1           # half width of the straight body sides
TOP_END_HALF_W = 18.25       # half width of the +Y end edge (both sides tapered)
TOP_TAPER_END = (23.0, 46.9)  # where the +Y end taper runs into the dome pads
BOT_LEFT_X = -19.15          # -Y end, left (straight) edge
BOT_SHELF_Y = -42.4          # -Y end, left: short shelf edge running into the dome foot
BOT_RIGHT_X = 22.8           # -Y end, right edge below the dome
BOT_RIGHT_TAPER = ((BOT_RIGHT_X, -47.3), (18.0, Y_BOT))  # -Y end, right tapered edge

# corner domes: hollow round tube elbows standing on the plate.  Each rises
# vertically from a round foot (open underneath) and bends inward along the plate
# diagonal so that its closed flat end face points inward and upward; that end
# cap carries a round hole.
DOME_FOOT_X = 22.95          # |x| of the elbow foot centres
DOME_FOOT_Y_TOP = 41.52      # y of the +Y foot centres
DOME_FOOT_Y_BOT = -36.87     # y of the -Y foot centres
DOME_R = 5.4                 # tube radius (= foot / face radius)
DOME_BEND_R = 8.25           # bend radius of the elbow centre line
DOME_BEND = 45.0             # bend angle (face normal elevation = 90 - bend)
FACE_HOLE_R = 3.0            # hole through the flat end cap
DOME_BORE_R = 4.7            # bore of the hollow elbow (open at the plate bottom)
DOME_CAP_T = 0.9             # thickness of the end cap carrying the face hole
PAD_R = 5.15                 # plate lobe under each elbow (kept inside the elbow)
PAD_SHIFT = 0.2              # pad centre shifted inward from the foot centre

EAR_X = 21.9                 # side ears with screw holes
EAR_Y = 21.8
EAR_R = 4.35

CONVEX_R = 2.2               # rounding of outside outline corners
NOTCH_R_TOP = 6.04           # concave notch between +Y dome pad and ear
NOTCH_R_BOT = 3.46           # concave notch between -Y dome pad and ear
EAR_FILLET_R = 2.85          # concave blend between ears and straight sides

HOLE_D = 2.3                 # small screw holes
CORNER_HOLES = [(-16.4, 55.75), (16.4, 55.75), (-16.4, -55.9), (16.4, -55.9)]
EAR_HOLES = [(sx * EAR_X, sy * EAR_Y) for sx in (-1, 1) for sy in (-1, 1)]

SLOT_W = 2.7                 # three long slots
SLOT_XS = [-8.75, 0.0, 8.75]
SLOT_Y0, SLOT_Y1 = -13.5, 13.6

SQUARE = (-2.25, 14.95, 17.75, 36.6)   # x0, y0, x1, y1 of the square window
CUT_R = 1.25                 # corner radius of the triangular / trapezoid cut-outs
SQUARE_R = 1.5               # corner radius of the square window

# ======================= helpers =======================
def inward(x, y):
    """unit vector (xy) along the plate diagonal pointing inward from a corner dome"""
    return (-math.copysign(1, x) / math.sqrt(2), -math.copysign(1, y) / math.sqrt(2))


DOME_FEET = [(sx * DOME_FOOT_X, fy) for sx in (-1, 1) for fy in (DOME_FOOT_Y_TOP, DOME_FOOT_Y_BOT)]
PADS = [(fx + PAD_SHIFT * inward(fx, fy)[0], fy + PAD_SHIFT * inward(fx, fy)[1]) for (fx, fy) in DOME_FEET]

# ======================= plate outline =======================
def _unit(vx, vy):
    l = math.hypot(vx, vy)
    return vx / l, vy / l


def tangent_circle(ca, ra, cb, rb, rf, side):
    """centre of a circle of radius rf touching circles (ca,ra) and (cb,rb) from outside;
    side=-1/+1 picks the solution on the -X/+X side of the line ca-cb"""
    da, db = ra + rf, rb + rf
    dx, dy = cb[0] - ca[0], cb[1] - ca[1]
    d = math.hypot(dx, dy)
    a = (da * da - db * db + d * d) / (2 * d)
    h = math.sqrt(max(da * da - a * a, 0.0))
    mx, my = ca[0] + a * dx / d, ca[1] + a * dy / d
    c1 = (mx + h * dy / d, my - h * dx / d)
    c2 = (mx - h * dy / d, my + h * dx / d)
    return c1 if (c1[0] - c2[0]) * side > 0 else c2


def slab(pts):
    return cq.Workplane("XY").polyline(pts).close().extrude(1.0)


def disk(c, r):
    return cq.Workplane("XY").center(*c).circle(r).extrude(1.0)


def outline_face():
    (ptx, pty), (pbx, pby) = PADS[0], PADS[1]          # -X pads (+Y, -Y)
    pts = [
        (-TOP_END_HALF_W, Y_TOP), (TOP_END_HALF_W, Y_TOP),
        TOP_TAPER_END, (-ptx, pty), (BODY_HALF_W, pty - 4.0),
        (BODY_HALF_W, pby + 4.0), (-pbx, pby), (BOT_RIGHT_X, pby),
        BOT_RIGHT_TAPER[0], BOT_RIGHT_TAPER[1],
        (BOT_LEFT_X, Y_BOT), (BOT_LEFT_X, BOT_SHELF_Y), (pbx - 0.4, BOT_SHELF_Y),
        (pbx, pby), (-BODY_HALF_W, pby + 4.0),
        (-BODY_HALF_W, pty - 4.0), (ptx, pty), (-TOP_TAPER_END[0], TOP_TAPER_END[1]),
    ]
    shape = slab(pts)
    for sx in (-1, 1):
        for (pad, ear, rn) in ((PADS[0], (-EAR_X, EAR_Y), NOTCH_R_TOP),
                               (PADS[1], (-EAR_X, -EAR_Y), NOTCH_R_BOT)):
            pc = (sx * abs(pad[0]), pad[1])
            ec = (sx * abs(ear[0]), ear[1])
            nc = tangent_circle(pc, PAD_R, ec, EAR_R, rn, sx)
            ua, ub = _unit(nc[0] - pc[0], nc[1] - pc[1]), _unit(nc[0] - ec[0], nc[1] - ec[1])
            ta = (pc[0] + PAD_R * ua[0], pc[1] + PAD_R * ua[1])
            tb = (ec[0] + EAR_R * ub[0], ec[1] + EAR_R * ub[1])
            inner = sx * (BODY_HALF_W - 1.0)
            bridge = slab([pc, ta, tb, ec, (inner, ec[1]), (inner, pc[1])]).cut(disk(nc, rn))
            shape = shape.cut(disk(nc, rn)).union(bridge)
            # concave fillet between the ear and the straight body side (towards y = 0)
            fx = sx * (BODY_HALF_W + EAR_FILLET_R)
            fy = ec[1] - math.copysign(
                math.sqrt((EAR_R + EAR_FILLET_R) ** 2 - (fx - ec[0]) ** 2), ec[1])
            ue = _unit(fx - ec[0], fy - ec[1])
            te = (ec[0] + EAR_R * ue[0], ec[1] + EAR_R * ue[1])
            fill = slab([(sx * BODY_HALF_W, fy), te, ec, (sx * BODY_HALF_W, ec[1])]).cut(disk((fx, fy), EAR_FILLET_R))
            shape = shape.union(fill)
    shape = shape.union(cq.Workplane("XY").pushPoints(PADS).circle(PAD_R).extrude(1.0))
    shape = shape.union(cq.Workplane("XY").pushPoints(EAR_HOLES).circle(EAR_R).extrude(1.0))
    w = shape.faces("<Z").val().outerWire()
    # round the convex corners of the outline (concave ones are left sharp)
    w = w.offset2D(-CONVEX_R, "arc")[0].offset2D(CONVEX_R, "arc")[0]
    return cq.Face.makeFromWires(w)


plate = cq.Workplane("XY").add(outline_face()).wires().toPending().extrude(T)

# ======================= cut-outs through the plate =======================
def rounded_poly(pts, r=CUT_R):
    sk = cq.Sketch().polygon(list(pts) + [pts[0]]).vertices().fillet(r)
    return cq.Workplane("XY").placeSketch(sk).extrude(T + 2).translate((0, 0, -1))


cutters = []
# trapezoid windows at both ends
cutters.append(rounded_poly([(-10.25, 54.55), (10.25, 54.55), (13.55, 45.5), (-13.55, 45.5)]))
cutters.append(rounded_poly([(-13.55, -45.4), (13.55, -45.4), (9.8, -54.5), (-9.8, -54.5)]))
# square window
x0, y0, x1, y1 = SQUARE
cutters.append(rounded_poly([(x0, y0), (x1, y0), (x1, y1), (x0, y1)], SQUARE_R))
# triangular lightening pockets (mirrored pairs + centre one)
tri_left = [
    [(-17.75, -5.3), (-17.75, -23.9), (-10.5, -14.5)],        # slim side triangle
    [(-9.2, -16.9), (-15.6, -27.35), (-2.2, -27.35)],        # upper row
    [(-10.3, -32.2), (-15.45, -42.5), (-4.35, -42.5)],       # lower row
]
for tri in tri_left:
    cutters.append(rounded_poly(tri))
    cutters.append(rounded_poly([(-x, y) for (x, y) in tri[::-1]]))
cutters.append(rounded_poly([(-7.1, -31.65), (7.1, -31.65), (0.0, -42.7)]))
# long slots
for sx in SLOT_XS:
    cutters.append(
        cq.Workplane("XY").center(sx, (SLOT_Y0 + SLOT_Y1) / 2)
        .slot2D(SLOT_Y1 - SLOT_Y0, SLOT_W, 90).extrude(T + 2).translate((0, 0, -1))
    )
# screw holes
cutters.append(
    cq.Workplane("XY").pushPoints(CORNER_HOLES + EAR_HOLES)
    .circle(HOLE_D / 2).extrude(T + 2).translate((0, 0, -1))
)
for c in cutters:
    plate = plate.cut(c)

# ======================= domes =======================
def elbow(px, py):
    """tube of radius DOME_R swept from the foot (vertical) through DOME_BEND degrees"""
    d = inward(px, py)
    c = cq.Vector(px + DOME_BEND_R * d[0], py + DOME_BEND_R * d[1], 0)   # bend centre
    k = cq.Vector(-d[1], d[0], 0)                                           # bend axis
    foot = cq.Face.makeFromWires(cq.Wire.makeCircle(DOME_R, cq.Vector(px, py, 0), cq.Vector(0, 0, 1)))
    return cq.Solid.revolve(foot, DOME_BEND, c, c + k)


def face_frame(px, py):
    d = inward(px, py)
    b = math.radians(DOME_BEND)
    rb = DOME_BEND_R
    centre = cq.Vector(px + rb * (1 - math.cos(b)) * d[0], py + rb * (1 - math.cos(b)) * d[1], rb * math.sin(b))
    normal = cq.Vector(math.sin(b) * d[0], math.sin(b) * d[1], math.cos(b))
    return centre, normal


result = plate
for (px, py) in DOME_FEET:
    result = result.union(cq.Workplane().add(elbow(px, py)))

# hollow out the elbows (bore open through the plate bottom) and drill the end caps
for (px, py) in DOME_FEET:
    d = inward(px, py)
    c = cq.Vector(px + DOME_BEND_R * d[0], py + DOME_BEND_R * d[1], 0)
    k = cq.Vector(-d[1], d[0], 0)
    bore_foot = cq.Face.makeFromWires(cq.Wire.makeCircle(DOME_BORE_R, cq.Vector(px, py, 0), cq.Vector(0, 0, 1)))
    bore = cq.Solid.revolve(bore_foot, DOME_BEND, c, c + k)
    bore = bore.fuse(cq.Solid.makeCylinder(DOME_BORE_R, 1.5, cq.Vector(px, py, -1.0), cq.Vector(0, 0, 1)))
    fc, fn = face_frame(px, py)
    # stop the bore DOME_CAP_T short of the flat face
    keep = cq.Workplane(cq.Plane(origin=fc - fn * DOME_CAP_T, xDir=cq.Vector(d[0], d[1], 0).cross(fn), normal=fn))
    bore = bore.cut(keep.rect(40, 40).extrude(20).val())
    result = result.cut(cq.Workplane().add(bore))
    hole = cq.Solid.makeCylinder(FACE_HOLE_R, 4.0, fc + fn * 1.0, fn * -1)
    result = result.cut(cq.Workplane().add(hole))

VIEW = {"azimuth": 45, "elevation": 26}
